import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_TEETH = 10            # tooth count
R_TIP = 60.0            # tip radius of the sprocket plates
R_FLANK_END = 0.762 * R_TIP   # radius where tooth flank meets the root chord
TIP_HALF_ANG = 1.77     # half angular width of the flat tooth tip (deg)
FLANK_END_ANG = 10.5    # angular offset of flank end from tooth axis (deg)
FLANK_MID = (0.1029 * R_TIP, 0.8815 * R_TIP)  # mid point of flank arc (tangential, radial)
FIRST_TOOTH_ANG = 90.0  # one tooth points along +Y

PLATE_T = 9.2           # thickness of each sprocket plate
GAP = 4.4               # gap between the two plates

HEX_R = 18.5            # circumradius of central hex (hub insert / plate hole)
HEX_CHAMFER = 3.0       # corner truncation of the hex insert inside the plates
SPACER_CHAMFER = 0.0    # corner truncation of the hex spacer between the plates (sharp)

BOLT_HEX_R = 3.05       # circumradius of the 6 hex (nut) holes
BOLT_HEX_PCR = 30.0     # pitch radius of the hex holes
SMALL_HOLE_D = 2.7      # small round holes
SMALL_HOLE_PCR = 19.6
INNER_HOLE_PCR = 14.9   # 3 holes through the hex insert
CENTER_HOLE_D = 2.5
NUT_R = 4.3             # flush hex nut at the top centre (circumradius, flat top)
NUT_H = 3.2

HUB_D = 26.2            # round hub below the plates
HUB_H = 13.6
RING_D = 20.2           # small step ring at the hub end
RING_H = 1.8
BORE_D = 11.0           # shaft bore in the hub
SET_SCREW_D = 4.4
SET_SCREW_Z = 0.4       # fraction of hub height from the hub top
SET_SCREW_ANG0 = -27.0  # first set screw direction (deg), 4 at 90 deg


def pol(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


def local(theta_deg, x_t, y_r):
    """tooth-local (tangential, radial) -> global XY"""
    a = math.radians(theta_deg)
    ux, uy = math.cos(a), math.sin(a)
    vx, vy = -math.sin(a), math.cos(a)
    return (y_r * ux + x_t * vx, y_r * uy + x_t * vy)


def sprocket_outline():
    pitch = 360.0 / N_TEETH
    wp = None
    for k in range(N_TEETH):
        th = FIRST_TOOTH_ANG + k * pitch
        e_r = pol(R_FLANK_END, th - FLANK_END_ANG)
        t_r = pol(R_TIP, th - TIP_HALF_ANG)
        t_l = pol(R_TIP, th + TIP_HALF_ANG)
        e_l = pol(R_FLANK_END, th + FLANK_END_ANG)
        m_r = local(th, -FLANK_MID[0], FLANK_MID[1])
        m_l = local(th, FLANK_MID[0], FLANK_MID[1])
        if wp is None:
            wp = cq.Workplane("XY").moveTo(*e_r)
        else:
            # root: arc concentric with the sprocket between adjacent flanks
            wp = wp.threePointArc(pol(R_FLANK_END, th - pitch / 2), e_r)
        wp = wp.threePointArc(m_r, t_r).lineTo(*t_l).threePointArc(m_l, e_l)
    th0 = FIRST_TOOTH_ANG
    e_r0 = pol(R_FLANK_END, th0 - FLANK_END_ANG)
    wp = wp.threePointArc(pol(R_FLANK_END, th0 - pitch / 2), e_r0)
    return wp.close()


def hexagon_pts(r, rot_deg):
    return [pol(r, rot_deg + 60 * i) for i in range(6)]


def chamfered_hex_pts(r, c, rot_deg):
    """hexagon with each corner truncated by c along the edges"""
    pts = []
    side = r  # side length of a regular hexagon equals circumradius
    f = c / side
    verts = hexagon_pts(r, rot_deg)
    for i in range(6):
        p = verts[i]
        prv = verts[i - 1]
        nxt = verts[(i + 1) % 6]
        a = (p[0] + (prv[0] - p[0]) * f, p[1] + (prv[1] - p[1]) * f)
        b = (p[0] + (nxt[0] - p[0]) * f, p[1] + (nxt[1] - p[1]) * f)
        pts += [a, b]
    return pts


def make_plate(z0):
    plate = sprocket_outline().extrude(PLATE_T).translate((0, 0, z0))
    cut = (
        cq.Workplane("XY").workplane(offset=z0 - 1)
        .polyline(hexagon_pts(HEX_R, 30)).close().extrude(PLATE_T + 2)
    )
    # hex nut holes
    for i in range(6):
        cx, cy = pol(BOLT_HEX_PCR, 30 + 60 * i)
        pts = [(cx + x, cy + y) for (x, y) in hexagon_pts(BOLT_HEX_R, 30)]
        cut = cut.union(
            cq.Workplane("XY").workplane(offset=z0 - 1)
            .polyline(pts).close().extrude(PLATE_T + 2)
        )
    holes = (
        cq.Workplane("XY").workplane(offset=z0 - 1)
        .pushPoints([pol(SMALL_HOLE_PCR, 60 * i) for i in range(6)])
        .circle(SMALL_HOLE_D / 2).extrude(PLATE_T + 2)
    )
    return plate.cut(cut).cut(holes)


z_bot = 0.0
z_top = PLATE_T + GAP
plate_bottom = make_plate(z_bot)
plate_top = make_plate(z_top)
H_TOTAL = 2 * PLATE_T + GAP

# hex hub insert through both plates + round hub below
insert = (
    cq.Workplane("XY")
    .polyline(chamfered_hex_pts(HEX_R, HEX_CHAMFER, 30)).close()
    .extrude(H_TOTAL)
)
spacer_pts = (chamfered_hex_pts(HEX_R, SPACER_CHAMFER, 30) if SPACER_CHAMFER > 0
              else hexagon_pts(HEX_R, 30))
spacer = (
    cq.Workplane("XY").workplane(offset=PLATE_T)
    .polyline(spacer_pts).close()
    .extrude(GAP)
)
insert = insert.union(spacer)
# (cylinders are turned so their seam edges sit on the rear side)
hub = (
    cq.Workplane("XY").workplane(offset=-HUB_H)
    .circle(HUB_D / 2).extrude(HUB_H)
    .rotate((0, 0, 0), (0, 0, 1), 135)
)
ring = (
    cq.Workplane("XY").workplane(offset=-HUB_H - RING_H)
    .circle(RING_D / 2).extrude(RING_H)
    .rotate((0, 0, 0), (0, 0, 1), 135)
)
hubpart = insert.union(hub).union(ring)

# shaft bore from below, small centre hole above
bore = (
    cq.Workplane("XY").workplane(offset=-HUB_H - RING_H - 1)
    .circle(BORE_D / 2).extrude(HUB_H + RING_H + 1)
    .rotate((0, 0, 0), (0, 0, 1), -45)
)
center_hole = (
    cq.Workplane("XY").workplane(offset=-1)
    .circle(CENTER_HOLE_D / 2).extrude(H_TOTAL + 2)
)
inner_holes = (
    cq.Workplane("XY").workplane(offset=-1)
    .pushPoints([pol(INNER_HOLE_PCR, 90 + 120 * i) for i in range(3)])
    .circle(SMALL_HOLE_D / 2).extrude(H_TOTAL + 2)
)
nut_pocket = (
    cq.Workplane("XY").workplane(offset=H_TOTAL - NUT_H)
    .polyline(hexagon_pts(NUT_R, 0)).close().extrude(NUT_H + 1)
)
hubpart = hubpart.cut(bore).cut(center_hole).cut(inner_holes).cut(nut_pocket)

# flush centre nut sitting in its hex pocket
nut = (
    cq.Workplane("XY").workplane(offset=H_TOTAL - NUT_H)
    .polyline(hexagon_pts(NUT_R, 0)).close().extrude(NUT_H)
    .cut(center_hole)
)

# radial set screw holes
zs = -HUB_H * SET_SCREW_Z
for i in range(4):
    ang = SET_SCREW_ANG0 + 90 * i
    d = pol(1.0, ang)
    ss = (
        cq.Workplane(cq.Plane(origin=(0, 0, zs), xDir=(-d[1], d[0], 0), normal=(d[0], d[1], 0)))
        .circle(SET_SCREW_D / 2).extrude(HUB_D)
    )
    hubpart = hubpart.cut(ss)

result = cq.Workplane("XY").newObject([
    cq.Compound.makeCompound([plate_bottom.val(), plate_top.val(), hubpart.val(), nut.val()])
])

VIEW = {"azimuth": 45, "elevation": 26}
